import math

import cadquery as cq

# Round coupling disc: a flat disc (axis along Y, front face towards -Y) with a
# cross-shaped drive cut-out in the middle, four through holes on a square
# pattern that are countersunk from the back face, and a round-bottom groove
# running vertically (along Z) across the whole back face.

# ---------------- driving dimensions (mm) ----------------
D = 100.0            # disc diameter
T = 7.3              # disc thickness (along Y)
CROSS_SPAN = 30.75   # tip-to-tip length of each cross arm
CROSS_W = 9.0        # width of the cross arms
HOLE_OFF = 23.3      # hole offset from centre in X and in Z (square pattern)
HOLE_D = 3.9         # through-hole diameter
CSK_D = 9.0          # countersink diameter on the back face
CSK_ANGLE = 90.0     # countersink included angle
GROOVE_W = 6.5       # width of the vertical back groove (full round bottom)
GROOVE_DEPTH = 6.6   # depth of the groove measured from the back face

# ---------------- derived values ----------------
R = D / 2.0
y_front = -T / 2.0
y_back = T / 2.0
EXTRA = 1.0          # tool overshoot for clean through-cuts
csk_tan = math.tan(math.radians(CSK_ANGLE / 2.0))
csk_depth = (CSK_D - HOLE_D) / 2.0 / csk_tan

# ---------------- base disc ----------------
# "XZ" workplane normal is -Y, so extruding from the back face goes to the front.
disc = (
    cq.Workplane("XZ", origin=(0, y_back, 0))
    .circle(R)
    .extrude(T)
    .rotate((0, 0, 0), (0, 1, 0), 90)   # move the cylinder seam into the groove
)

# ---------------- central cross cut-out (through) ----------------
a = CROSS_SPAN / 2.0
b = CROSS_W / 2.0
cross_pts = [
    (a, b), (b, b), (b, a), (-b, a), (-b, b), (-a, b),
    (-a, -b), (-b, -b), (-b, -a), (b, -a), (b, -b), (a, -b),
]
cross = (
    cq.Workplane("XZ", origin=(0, y_back + EXTRA, 0))
    .polyline(cross_pts)
    .close()
    .extrude(T + 2 * EXTRA)
)
disc = disc.cut(cross)

# ---------------- four through holes, countersunk from the back ----------------
# Half profile in the local (Y, Z) plane of a "YZ" workplane placed on the hole
# axis, revolved 360 deg about that axis (local x == global Y).
hole_prof = [
    (y_front - EXTRA, 0.0),
    (y_front - EXTRA, HOLE_D / 2.0),
    (y_back - csk_depth, HOLE_D / 2.0),
    (y_back + EXTRA, CSK_D / 2.0 + EXTRA * csk_tan),
    (y_back + EXTRA, 0.0),
]
for sx in (-1, 1):
    for sz in (-1, 1):
        tool = (
            cq.Workplane("YZ", origin=(sx * HOLE_OFF, 0, sz * HOLE_OFF))
            .polyline(hole_prof)
            .close()
            .revolve(360, (0, 0, 0), (1, 0, 0))
        )
        disc = disc.cut(tool)

# ---------------- vertical round-bottom groove on the back face ----------------
# U-shaped profile drawn in the XY plane (x across, y through the thickness),
# extruded along Z through the full diameter.
gr = GROOVE_W / 2.0
y_arc = y_back - GROOVE_DEPTH + gr        # centre of the round bottom
groove = (
    cq.Workplane("XY", origin=(0, 0, -R - EXTRA))
    .moveTo(-gr, y_back + EXTRA)
    .lineTo(-gr, y_arc)
    .threePointArc((0, y_arc - gr), (gr, y_arc))
    .lineTo(gr, y_back + EXTRA)
    .close()
    .extrude(D + 2 * EXTRA)
)
disc = disc.cut(groove)

result = disc

VIEW = {"azimuth": 45, "elevation": 26}
